import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
BAND_T = 2.0          # thickness of the head band ribbon
BAND_H = 7.5          # height of band / brim plate
LIP_TOP = 21.0        # top of the raised forehead lip (from underside)
LIP_LEAN = 8.2        # inward lean of the forehead wall (top vs its foot)
LIP_TOP_W = 2.4       # width of the flat top of the wall
RAMP_OUT = 3.2        # foot of the wall's outer face, from band centre
RAISE_END_Y = 44.0    # where the raised lip ends on the sides
RAISE_END_R = 5.0     # length of the elliptic roll-off at the wall ends
RAISE_END_H = 6.7     # height of the elliptic roll-off
HOOK_R = 2.2          # centre-line radius of the end hooks
HOOK_ANGLE = 165.0    # wrap angle of the end hooks (deg)
STUD_R = 4.2          # radius of the round shield pegs
STUD_NECK = 1.6       # straight part of the pegs before the domed end
EAR_R = 11.7          # radius of the D-shaped ear tabs
EAR_T = 2.0           # thickness of the ear tabs
EAR_C = (78.0, -73.2) # ear tab centre (right side, mirrored)
SLOT_U = (1.0, 3.6)   # underside shield slot, offsets from band centre
SLOT_D = 5.0          # slot depth
SLOT_END_Y = 62.0     # slot ends on the sides

# band centre line, left half, from front centre to the back end
BAND_LEFT = [
    (0.0, 96.8), (-24.8, 95.6), (-39.6, 93.0), (-51.3, 89.5), (-61.1, 85.1),
    (-69.4, 80.0), (-76.2, 74.5), (-81.7, 69.2), (-86.2, 63.5), (-90.3, 57.6),
    (-94.0, 51.5), (-96.8, 44.5), (-98.2, 37.0), (-99.0, 27.0), (-99.5, 15.0),
    (-99.6, 3.0), (-98.9, -8.0), (-97.4, -18.0), (-95.0, -28.0),
    (-92.3, -38.0), (-89.0, -47.0), (-80.0, -68.0), (-66.0, -88.0),
    (-48.0, -103.0), (-30.5, -113.5),
]
# brim outer contour, left half, from front centre to where it merges the band
BRIM_LEFT = [
    (0.0, 116.3), (-15.0, 115.7), (-30.0, 114.1), (-45.0, 112.2), (-58.0, 109.2),
    (-78.5, 101.8),
    (-90.5, 94.3), (-97.0, 83.0), (-100.8, 65.0), (-102.5, 42.0),
    (-103.1, 22.0), (-102.6, 3.0), (-100.4, -12.0), (-97.6, -24.0),
]
FRONT_STUD = (49.6, 111.4)   # on brim outer contour (right side)
SIDE_STUD = (103.2, 33.7)


def V(x, y, z=0.0):
    return cq.Vector(x, y, z)


def full_path(left):
    pts = list(reversed(left))                 # back-left ... front
    pts += [(-x, y) for (x, y) in left[1:]]     # front ... back-right
    return pts


# ---------------- band centre line ----------------
band_pts = full_path(BAND_LEFT)
band_edge = cq.Edge.makeSpline([V(*p) for p in band_pts])

t0 = band_edge.tangentAt(0.0)
t1 = band_edge.tangentAt(1.0)
p0 = band_edge.startPoint()
p1 = band_edge.endPoint()


def hook_edge(p, d, right_side):
    """tight arc curling outwards at the end of an arm.
    p = arm end point, d = unit direction of travel leaving the arm."""
    d = cq.Vector(d.x, d.y, 0).normalized()
    if right_side:
        n = cq.Vector(-d.y, d.x, 0)
    else:
        n = cq.Vector(d.y, -d.x, 0)
    c = p + n * HOOK_R
    a0 = math.atan2(p.y - c.y, p.x - c.x)
    sgn = 1.0 if right_side else -1.0
    am = a0 + sgn * math.radians(HOOK_ANGLE) / 2
    a1 = a0 + sgn * math.radians(HOOK_ANGLE)
    pm = V(c.x + HOOK_R * math.cos(am), c.y + HOOK_R * math.sin(am))
    pe = V(c.x + HOOK_R * math.cos(a1), c.y + HOOK_R * math.sin(a1))
    return cq.Edge.makeThreePointArc(p, pm, pe)


def sweep_profile(edge, prof_uv):
    """sweep a closed (u,z) profile along a planar path; u = outward normal"""
    w = cq.Wire.assembleEdges([edge])
    st = edge.startPoint()
    tg = edge.tangentAt(0.0).normalized()
    outward = cq.Vector(-tg.y, tg.x, 0).normalized()
    pl = cq.Plane(origin=st, xDir=outward, normal=tg)
    prof = cq.Workplane(pl).polyline(prof_uv).close()
    return prof.sweep(cq.Workplane().add(w), transition="right")


def closed_face_solid(pts2d, z0, z1):
    """spline through pts closed by a straight line, extruded z0..z1"""
    pts = [V(x, y, z0) for (x, y) in pts2d]
    sp = cq.Edge.makeSpline(pts)
    ln = cq.Edge.makeLine(pts[-1], pts[0])
    w = cq.Wire.assembleEdges([sp, ln])
    f = cq.Face.makeFromWires(w)
    return cq.Workplane().add(cq.Solid.extrudeLinear(f, cq.Vector(0, 0, z1 - z0)))


# region enclosed by the band centre line (the head opening)
head = closed_face_solid(band_pts, -5.0, LIP_TOP + 5.0)
head_solid = head.val()

# ---------------- band + brim as one extruded outline ----------------
# inner face of the band: offset of the centre line (single smooth B-spline)
def offset_spline(edge, d, n=120):
    pts = []
    for k in range(n + 1):
        s = k / n
        q = edge.positionAt(s)
        tg = edge.tangentAt(s).normalized()
        pts.append(V(q.x - tg.y * d, q.y + tg.x * d, 0.0))
    return cq.Edge.makeSplineApprox(pts, tol=0.002, minDeg=3, maxDeg=6)


inner_edge = offset_spline(band_edge, -BAND_T / 2)
nL = cq.Vector(-t0.y, t0.x, 0).normalized()   # outward normal at left end
nR = cq.Vector(-t1.y, t1.x, 0).normalized()   # outward normal at right end
oL = p0 + nL * (BAND_T / 2)
oR = p1 + nR * (BAND_T / 2)
iL = inner_edge.startPoint()
iR = inner_edge.endPoint()

# outer outline: arm outer face flaring into the brim contour and back
arm_back = []
for (x, y) in BAND_LEFT[-5:-1]:
    arm_back.append((x, y))
brim_left = list(BRIM_LEFT)
# offset the arm centre-line points to the outer face
arm_outer = []
for (x, y) in arm_back:
    # parameter of nearest point on the centre line
    best_s, best_d = 0.0, 1e9
    for k in range(0, 401):
        s = k / 400.0
        q = band_edge.positionAt(s)
        d = (q.x - x) ** 2 + (q.y - y) ** 2
        if d < best_d:
            best_s, best_d = s, d
    q = band_edge.positionAt(best_s)
    tg = band_edge.tangentAt(best_s).normalized()
    n = cq.Vector(-tg.y, tg.x, 0)
    arm_outer.append((q.x + n.x * BAND_T / 2, q.y + n.y * BAND_T / 2))
left_outer = brim_left + arm_outer              # front -> back (left side)
outer_pts = [oL] + [V(x, y) for (x, y) in reversed(left_outer)]
outer_pts += [V(-x, y) for (x, y) in left_outer[1:]] + [oR]
outer_spline = cq.Edge.makeSpline(outer_pts, tangents=[t0, t1])

outline = cq.Wire.assembleEdges(
    [outer_spline, cq.Edge.makeLine(oR, iR), inner_edge, cq.Edge.makeLine(iL, oL)])
band = cq.Workplane().add(
    cq.Solid.extrudeLinear(cq.Face.makeFromWires(outline), cq.Vector(0, 0, BAND_H)))

# hooks at both ends
slab = cq.Workplane().box(400, 400, BAND_H, centered=(True, True, False))
for he in (hook_edge(p1, t1, True), hook_edge(p0, -t0, False)):
    hw = cq.Wire.assembleEdges([he])
    st = he.startPoint()
    tg = he.tangentAt(0.0).normalized()
    outward = cq.Vector(-tg.y, tg.x, 0).normalized()
    pl = cq.Plane(origin=st, xDir=outward, normal=tg)
    hs = cq.Workplane(pl).rect(BAND_T, BAND_H * 2, centered=True).sweep(cq.Workplane().add(hw))
    band = band.union(hs.intersect(slab))

outer_region = cq.Workplane().add(cq.Solid.extrudeLinear(
    cq.Face.makeFromWires(cq.Wire.assembleEdges([outer_spline, cq.Edge.makeLine(oR, oL)])),
    cq.Vector(0, 0, LIP_TOP + 1.0)))

# ---------------- raised forehead lip with sloped ramp ----------------
u_b = BAND_T / 2          # the wall rises from the outer edge of the band top
ramp_prof = [
    (u_b, BAND_H * 0.5),
    (RAMP_OUT + 0.6, BAND_H * 0.5),
    (RAMP_OUT, BAND_H),
    (u_b - LIP_LEAN + LIP_TOP_W, LIP_TOP),
    (u_b - LIP_LEAN, LIP_TOP),
    (u_b, BAND_H),
]
ramp = sweep_profile(band_edge, ramp_prof)
plan_env = outer_region.union(head)
ramp = ramp.intersect(plan_env)
# side envelope: keep Y >= RAISE_END_Y; the wall ends with a steep face that
# rolls over into the top along a quarter ellipse
_zv = LIP_TOP - RAISE_END_H
side_env = (
    cq.Workplane("XY")
    .box(300, 200, LIP_TOP + 1.0, centered=(True, False, False))
    .translate((0, RAISE_END_Y + RAISE_END_R, -1.0))
    .union(cq.Workplane("XY").box(300, RAISE_END_R + 1.0, _zv + 1.0, centered=(True, False, False))
           .translate((0, RAISE_END_Y, -1.0)))
    .union(cq.Workplane("YZ").center(RAISE_END_Y + RAISE_END_R, _zv)
           .ellipse(RAISE_END_R, RAISE_END_H).extrude(150.0, both=True))
)
ramp = ramp.intersect(side_env)

body = band.union(ramp)

# ---------------- shield slot in the brim underside ----------------
slot = sweep_profile(band_edge, [(SLOT_U[0], -1.0), (SLOT_U[1], -1.0),
                                 (SLOT_U[1], SLOT_D), (SLOT_U[0], SLOT_D)])
slot = slot.intersect(
    cq.Workplane().box(400, 200, 50, centered=(True, False, True)).translate((0, SLOT_END_Y, 0)))
body = body.cut(slot)

# ---------------- shield studs (round pegs with domed ends, flush top) ----------------
def stud_at(px, py, nx, ny):
    n = cq.Vector(nx, ny, 0).normalized()
    base = V(px, py, BAND_H / 2) - n * 2.0
    tip_c = V(px, py, BAND_H / 2) + n * STUD_NECK
    peg = cq.Solid.makeCylinder(STUD_R, STUD_NECK + 2.0, base, n)
    dome = cq.Solid.makeSphere(STUD_R, tip_c, n, angleDegrees1=0, angleDegrees2=90)
    return cq.Workplane().add(peg).union(cq.Workplane().add(dome)).intersect(slab)


for sx in (1, -1):
    body = body.union(stud_at(sx * FRONT_STUD[0], FRONT_STUD[1], sx * 0.12, 1.0))
    body = body.union(stud_at(sx * SIDE_STUD[0], SIDE_STUD[1], sx * 1.0, 0.0))

# ---------------- D-shaped ear tabs ----------------
for sx in (1, -1):
    tab = cq.Workplane().center(sx * EAR_C[0], EAR_C[1]).circle(EAR_R).extrude(EAR_T)
    body = body.union(tab.cut(head))

result = body
